import math
import cadquery as cq
from OCP.TopExp import TopExp
from OCP.TopTools import TopTools_IndexedDataMapOfShapeListOfShape
from OCP.TopAbs import TopAbs_EDGE, TopAbs_FACE

# ---------------- driving dimensions (mm) ----------------
W = 31.95       # overall X (block length incl. plate)
L = 47.3        # overall Y (plate length)
T = 10.7        # plate thickness (X)
D = 13.0        # block depth (Y)
HB = 28.7       # block height (Z)
RT = 10.55      # plate top corner radius (= plate rise above block)
RC = 8.5        # big vertical corner radius (front / +X)
RE = 0.45       # small edge round on outer edges

# block top counterbored holes (vertical, through)
BH_X = (6.85, 17.56)
BH_D = 5.8
BH_CB_D = 9.7
BH_CB_DEPTH = 3.35

# plate holes
PH_Y = 28.35
PH_Z = 31.45
PH_D = 5.7
PH_CB_D = 9.7
PH_CB_DEPTH = 5.5
PIN_D = 4.5
PIN_DEPTH = 5.0
PIN_DY = 9.45

# slots in the plate (through, counterbored from the inner -X face)
SL_Y = (18.9, 37.8)
SL_Z0 = 4.5
SL_Z1 = 24.4
SL_W = 5.7
SL_CB_W = 9.7
SL_CB_DEPTH = 4.0

# embossed lettering on the block end face (reads upward along +Z)
TXT_SIZE = 12.0
TXT_H = 1.1
TXT_Y = 5.65
# (letter, centre Z, stretch along reading direction)
LETTERS = (("z", 5.0, 1.12), ("e", 11.6, 1.0), ("r", 17.7, 1.0), ("o", 22.95, 1.0))
CB_ROUND = 0.5   # round on block counterbore mouths
PH_CB_ROUND = 0.8  # round on plate counterbore mouth
RJ = 0.35       # concave round where the plate arc meets the block top

VIEW = {"azimuth": 45, "elevation": 26}


def sharp_edges(shape, min_angle=15.0):
    """Edges whose two adjacent faces meet at an angle (not tangent)."""
    m = TopTools_IndexedDataMapOfShapeListOfShape()
    TopExp.MapShapesAndAncestors_s(shape.wrapped, TopAbs_EDGE, TopAbs_FACE, m)
    out = []
    for i in range(1, m.Extent() + 1):
        e = cq.Edge(m.FindKey(i))
        faces = [cq.Face(f) for f in m.FindFromIndex(i)]
        if len(faces) != 2:
            continue
        p = e.positionAt(0.5)
        n1 = faces[0].normalAt(p)
        n2 = faces[1].normalAt(p)
        c = max(-1.0, min(1.0, n1.dot(n2)))
        if math.degrees(math.acos(c)) > min_angle:
            out.append(e)
    return out


# ---------------- plate (profile in YZ, extruded along X) ----------------
x0 = W - T
plate = (
    cq.Workplane("YZ", origin=(x0, 0, 0))
    .moveTo(0, 0)
    .lineTo(L, 0)
    .lineTo(L, HB)
    .radiusArc((L - RT, HB + RT), -RT)
    .lineTo(D + RT, HB + RT)
    .radiusArc((D, HB), -RT)
    .lineTo(0, HB)
    .close()
    .extrude(T)
)

block = cq.Workplane("XY").box(W, D, HB, centered=False)

body = plate.union(block)

# big rounded vertical corner at front (+X, -Y)
body = body.edges(cq.selectors.NearestToPointSelector((W, 0, HB / 2))).fillet(RC)

# small rounds on all remaining sharp outer edges
solid = body.val()
_round = []
for e in sharp_edges(solid):
    c = e.Center()
    # leave the edges that run into the plate/block inner junction sharp
    if abs(c.y - D) < 1e-3 and (abs(c.x - x0) < 1e-3 or abs(c.z - HB) < 1e-3):
        continue
    # the lettered end face (-X) keeps crisp edges
    if abs(c.x) < 1e-3:
        continue
    _round.append(e)
try:
    solid = solid.fillet(RE, _round)
except Exception:
    pass
# small concave round between block top and the rising plate arc
try:
    _j = [e for e in solid.Edges()
          if abs(e.Center().y - D) < 1e-3 and abs(e.Center().z - HB) < 1e-3
          and e.Center().x > x0 + 1e-3]
    solid = solid.fillet(RJ, _j)
except Exception:
    pass
body = cq.Workplane("XY").add(solid)

# ---------------- block top counterbored holes ----------------
for bx in BH_X:
    c = (
        cq.Workplane("XY", origin=(bx, D / 2, HB - BH_CB_DEPTH))
        .circle(BH_CB_D / 2).extrude(BH_CB_DEPTH + 1)
        .union(cq.Workplane("XY", origin=(bx, D / 2, -1)).circle(BH_D / 2).extrude(HB + 2))
    )
    body = body.cut(c)

# ---------------- plate through hole (counterbore on +X) ----------------
h = (
    cq.Workplane("YZ", origin=(x0 - 1, 0, 0)).center(PH_Y, PH_Z)
    .circle(PH_D / 2).extrude(T + 2)
    .union(
        cq.Workplane("YZ", origin=(W - PH_CB_DEPTH, 0, 0)).center(PH_Y, PH_Z)
        .circle(PH_CB_D / 2).extrude(PH_CB_DEPTH + 1)
    )
)
body = body.cut(h)

# blind pin holes from the inner -X face, above the slots
for dy in (-PIN_DY, PIN_DY):
    p = (
        cq.Workplane("YZ", origin=(x0 - 1, 0, 0)).center(PH_Y + dy, PH_Z)
        .circle(PIN_D / 2).extrude(PIN_DEPTH + 1)
    )
    body = body.cut(p)

# ---------------- slots (through, counterbored on -X face) ----------------
for sy in SL_Y:
    zc = (SL_Z0 + SL_Z1) / 2
    ln = SL_Z1 - SL_Z0
    s = (
        cq.Workplane("YZ", origin=(x0 - 1, 0, 0)).center(sy, zc)
        .slot2D(ln, SL_W, 90).extrude(T + 2)
    )
    scb = (
        cq.Workplane("YZ", origin=(x0 - 1, 0, 0)).center(sy, zc)
        .slot2D(ln + (SL_CB_W - SL_W), SL_CB_W, 90).extrude(SL_CB_DEPTH + 1)
    )
    body = body.cut(s).cut(scb)

# ---------------- rounded counterbore mouths ----------------
_mouths = [((bx, D / 2, HB), CB_ROUND) for bx in BH_X] + [((W, PH_Y, PH_Z), PH_CB_ROUND)]
for pt, r in _mouths:
    try:
        body = body.edges(cq.selectors.NearestToPointSelector(pt)).fillet(r)
    except Exception:
        pass

# ---------------- embossed text on the -X end face ----------------
for ch, zc, stretch in LETTERS:
    try:
        g = cq.Workplane("XY").text(ch, TXT_SIZE, TXT_H + 0.2, combine=False,
                                    halign="center", valign="center").val()
        if stretch != 1.0:
            g = g.transformGeometry(cq.Matrix([[stretch, 0, 0, 0], [0, 1, 0, 0], [0, 0, 1, 0]]))
        bb = g.BoundingBox()
        g = g.translate(cq.Vector(-(bb.xmin + bb.xmax) / 2, -(bb.ymin + bb.ymax) / 2, -0.2))
        # local x (reading) -> +Z, local y (letter up) -> +Y, local z (relief) -> -X
        g = g.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), -90)
        g = g.translate(cq.Vector(0, TXT_Y, zc))
        if g.isValid():
            body = body.union(cq.Workplane("XY").add(g))
    except Exception:
        pass

result = body
